import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BODY_D = 100.0          # main cylindrical body diameter
FLANGE_D = 107.6        # bottom flange diameter
FLANGE_T = 5.15         # flange thickness
TOTAL_H = 36.4          # overall height
SEAM_ANGLE = 47.0       # angular position of the cylinder seams (cosmetic only)

HOLE_D = 18.8           # two through holes
HOLE_Y = 35.7           # hole centre offset from axis (along Y)

# central through window (TV-screen like outline)
WIN_A = 44.0            # half length (X) at the middle of the short sides
WIN_B = 21.4            # half width (Y) at the middle of the long sides
WIN_FLAT = 31.0         # half length of the straight part of the long sides
WIN_R_LONG = 25.0       # radius rolling the long side down into the corner
WIN_R_CORNER = 5.0      # corner radius
WIN_R_SIDE = 150.0      # bulge radius of the short sides

SLOT_L = 7.5            # small blind slots (4 per hole)
SLOT_W = 3.2
SLOT_DEPTH = 1.8
SLOT_FLOOR_R = 1.8      # quarter round rolling the floor up to one long edge
SLOT_DX = 17.0          # x offset of slot centre from hole centre
SLOT_DY = 3.4           # y offset of slot centre from pair centre line
SLOT_SHIFT = 0.3        # pair centre line sits this much closer to the part axis than the hole


# ---------------- helpers ----------------
def circle_intersection(c1, r1, c2, r2):
    dx, dy = c2[0] - c1[0], c2[1] - c1[1]
    d = math.hypot(dx, dy)
    a = (r1 ** 2 - r2 ** 2 + d ** 2) / (2 * d)
    h = math.sqrt(max(r1 ** 2 - a ** 2, 0.0))
    px, py = c1[0] + a * dx / d, c1[1] + a * dy / d
    return [(px + h * dy / d, py - h * dx / d), (px - h * dy / d, py + h * dx / d)]


def on_circle(c, r, toward):
    vx, vy = toward[0] - c[0], toward[1] - c[1]
    n = math.hypot(vx, vy)
    return (c[0] + r * vx / n, c[1] + r * vy / n)


def arc_mid(c, r, p, q):
    a1 = math.atan2(p[1] - c[1], p[0] - c[0])
    a2 = math.atan2(q[1] - c[1], q[0] - c[0])
    da = math.atan2(math.sin(a2 - a1), math.cos(a2 - a1))
    am = a1 + da / 2.0
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


# ---------------- window outline (quadrant 1, then mirrored) ----------------
C1 = (WIN_FLAT, WIN_B - WIN_R_LONG)          # centre of long-side roll arc
C3 = (WIN_A - WIN_R_SIDE, 0.0)               # centre of short-side bulge arc
cands = circle_intersection(C1, WIN_R_LONG - WIN_R_CORNER, C3, WIN_R_SIDE - WIN_R_CORNER)
CC = max(cands, key=lambda p: p[1])          # corner arc centre
T1 = on_circle(C1, WIN_R_LONG, CC)           # long roll arc -> corner
T3 = on_circle(C3, WIN_R_SIDE, CC)           # corner -> short side

P0 = (WIN_FLAT, WIN_B)
M01 = arc_mid(C1, WIN_R_LONG, P0, T1)
MC = arc_mid(CC, WIN_R_CORNER, T1, T3)


def mx(p):
    return (-p[0], p[1])


def my(p):
    return (p[0], -p[1])


win = (
    cq.Workplane("XY")
    .moveTo(*mx(P0))
    .lineTo(*P0)
    .threePointArc(M01, T1)
    .threePointArc(MC, T3)
    .threePointArc((WIN_A, 0.0), my(T3))
    .threePointArc(my(MC), my(T1))
    .threePointArc(my(M01), my(P0))
    .lineTo(*mx(my(P0)))
    .threePointArc(mx(my(M01)), mx(my(T1)))
    .threePointArc(mx(my(MC)), mx(my(T3)))
    .threePointArc((-WIN_A, 0.0), mx(T3))
    .threePointArc(mx(MC), mx(T1))
    .threePointArc(mx(M01), mx(P0))
    .close()
)

# ---------------- base body (flange + cylinder) ----------------
body = (
    cq.Workplane("XY")
    .circle(FLANGE_D / 2.0).extrude(FLANGE_T)
    .faces(">Z").workplane()
    .circle(BODY_D / 2.0).extrude(TOTAL_H - FLANGE_T)
    # turn the (invisible, purely topological) cylinder seams to the back
    .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
)

# central through window
window = win.extrude(TOTAL_H + 2.0).translate((0, 0, -1.0))
body = body.cut(window)

# ---------------- two through holes ----------------
holes = (
    cq.Workplane("XY").workplane(offset=-1.0)
    .pushPoints([(0, HOLE_Y), (0, -HOLE_Y)])
    .circle(HOLE_D / 2.0)
    .extrude(TOTAL_H + 2.0)
)
body = body.cut(holes)

# ---------------- small blind slots ----------------
# Each pair of slots is mirror-symmetric about the line through the hole
# centre: the floor of every slot rolls up (quarter round) on the long edge
# facing the other slot of the pair.
def slot_tool(cx, cy, round_side):
    """round_side = +1 -> floor rounded on the +Y long edge, -1 -> on -Y."""
    z0 = TOTAL_H - SLOT_DEPTH
    # cross-section in the YZ plane, extruded along X over the slot length
    tool = (
        cq.Workplane("YZ", origin=(cx - SLOT_L / 2.0, 0, 0))
        .center(cy, z0 + (SLOT_DEPTH + 1.0) / 2.0)
        .rect(SLOT_W, SLOT_DEPTH + 1.0)
        .extrude(SLOT_L)
    )
    sel = ">Y" if round_side > 0 else "<Y"
    return tool.faces("<Z").edges(sel).fillet(SLOT_FLOOR_R)


slots = None
for hy in (HOLE_Y, -HOLE_Y):
    for sx in (-SLOT_DX, SLOT_DX):
        for sy in (-SLOT_DY, SLOT_DY):
            # the rounded edge faces the hole-centre line (the gap of the pair)
            cy = hy - math.copysign(SLOT_SHIFT, hy) + sy
            tool = slot_tool(sx, cy, -1 if sy > 0 else 1)
            slots = tool if slots is None else slots.union(tool)
body = body.cut(slots)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
